import cadquery as cq
from cadquery import selectors as sel

# ---------------- driving dimensions (mm) ----------------
PCB_W = 13.2        # along X
PCB_H = 17.1        # along Z
PCB_T = 1.35        # along Y (front face at Y=0, back face at Y=PCB_T)

SMALL_D = 1.0
BIG_D = 2.1
SMALL_HOLES = [(3.28, 12.11), (1.98, 10.04), (1.96, 4.33), (3.28, 1.21)]
BIG_HOLES = [(4.82, 4.12)]

PITCH = 2.54
PIN_W = 0.55
PIN_Z = 15.27         # height of horizontal pin run
PIN_FRONT = 1.5       # stub length in front of the PCB
PIN_BEND_Y = 5.17     # Y of the vertical pin leg (centre)
PIN_TOP = 21.67       # top of vertical pin legs
PIN_R_OUT = 0.25      # bend rounding (outer)
PIN_R_IN = 0.10       # bend rounding (inner)

HDR_SEG_W = 2.14      # header plastic segment width (X)
HDR_SEG_PITCH = 2.18
HDR_D = 2.54          # header depth (Y)
HDR_Z0, HDR_Z1 = 14.2, 16.35
HDR_R = 0.30          # rounding of the top edges of each segment

CYL_D = 5.2
CYL_Y = PCB_T + CYL_D / 2.0
CYL_TOP = 4.87
NECK_TOP, NECK_BOT = 1.83, 0.93
NECK_D = 4.15
CYL_BOT = -3.85
CYL_R = 0.15          # small edge rounding at the neck
CYL_RB = 0.22         # rounding of the bottom outer edge
RECESS_D = 2.6
RECESS_DEPTH = 1.0

SEAM_ANG = 90.0     # angular position of the revolve seam

TAB_T = 0.69
TAB_Y1 = 6.88
TAB_TOP = 8.21


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


class CircleEdgeSel(cq.Selector):
    """Select circular edges of a given radius lying at a given height."""

    def __init__(self, r, z, tol=1e-3):
        self.r, self.z, self.tol = r, z, tol

    def filter(self, objectList):
        out = []
        for e in objectList:
            if e.geomType() != "CIRCLE":
                continue
            if abs(e.radius() - self.r) < self.tol and abs(e.Center().z - self.z) < self.tol:
                out.append(e)
        return out


# ---------------- PCB ----------------
pcb = box(-PCB_W / 2, PCB_W / 2, 0, PCB_T, 0, PCB_H)
pts_small = []
for (x, z) in SMALL_HOLES:
    pts_small += [(x, z), (-x, z)]
pts_big = []
for (x, z) in BIG_HOLES:
    pts_big += [(x, z), (-x, z)]

# XZ workplane normal is -Y; local x = X, local y = Z
cut_small = (cq.Workplane("XZ").workplane(offset=1.0)
             .pushPoints(pts_small).circle(SMALL_D / 2).extrude(-(PCB_T + 2)))
cut_big = (cq.Workplane("XZ").workplane(offset=1.0)
           .pushPoints(pts_big).circle(BIG_D / 2).extrude(-(PCB_T + 2)))
pcb = pcb.cut(cut_small).cut(cut_big)

# ---------------- header (plastic segments + bent pins) ----------------
hdr = None
for i in (-1, 0, 1):
    cx = i * HDR_SEG_PITCH
    seg = box(cx - HDR_SEG_W / 2, cx + HDR_SEG_W / 2,
              PCB_T, PCB_T + HDR_D, HDR_Z0, HDR_Z1)
    seg = seg.edges("|Y").edges(">Z").edges(">X").fillet(HDR_R)
    hdr = seg if hdr is None else hdr.union(seg)

h = PIN_W / 2
pins = None
for i in (-1, 0, 1):
    px = i * PITCH
    # L-shaped profile in the YZ plane (local x = Y, local y = Z)
    prof = [
        (-PIN_FRONT, PIN_Z - h),
        (PIN_BEND_Y + h, PIN_Z - h),
        (PIN_BEND_Y + h, PIN_TOP),
        (PIN_BEND_Y - h, PIN_TOP),
        (PIN_BEND_Y - h, PIN_Z + h),
        (-PIN_FRONT, PIN_Z + h),
    ]
    p = (cq.Workplane("YZ").workplane(offset=px - h)
         .polyline(prof).close().extrude(PIN_W))
    p = p.edges(sel.NearestToPointSelector((px, PIN_BEND_Y + h, PIN_Z - h))).fillet(PIN_R_OUT)
    p = p.edges(sel.NearestToPointSelector((px, PIN_BEND_Y - h, PIN_Z + h))).fillet(PIN_R_IN)
    pins = p if pins is None else pins.union(p)

# ---------------- cylindrical component with tab ----------------
R = CYL_D / 2.0
RN = NECK_D / 2.0
RR = RECESS_D / 2.0
prof = [
    (0, CYL_TOP), (R, CYL_TOP), (R, NECK_TOP), (RN, NECK_TOP),
    (RN, NECK_BOT), (R, NECK_BOT), (R, CYL_BOT), (RR, CYL_BOT),
    (RR, CYL_BOT + RECESS_DEPTH), (0, CYL_BOT + RECESS_DEPTH),
]
comp = (cq.Workplane("XZ").polyline(prof).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
for zc in (NECK_TOP, NECK_BOT):
    comp = comp.edges(CircleEdgeSel(R, zc)).fillet(CYL_R)
comp = comp.edges(CircleEdgeSel(R, CYL_BOT)).fillet(CYL_RB)
comp = comp.rotate((0, 0, 0), (0, 0, 1), SEAM_ANG).translate((0, CYL_Y, 0))
tab = box(-TAB_T / 2, TAB_T / 2, PCB_T, TAB_Y1, CYL_TOP, TAB_TOP)
comp = comp.union(tab)

result = pcb.union(hdr).union(pins).union(comp)

VIEW = {"azimuth": 45, "elevation": 26}
